"""Tapered ridge cover / end cap.

A hollow, tapering 'roof' shaped shell: the section is a trapezoid with a
constant-width ridge cap on top.  Width and height both halve from the closed
front end to the open back end.  The shell is open at the bottom and at the back,
the ridge cap is solid, and the front wall carries a horizontal snap slot with a
shallow guide groove running up to it on the inside.
"""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H0 = 60.0         # ridge height at the front (closed) end
W0 = 60.0         # base width at the front end
H1 = 30.0         # ridge height at the back (open) end
W1 = 30.0         # base width at the back end
L = 115.0         # length, front -> back
ROOF_HALF = 6.85  # half width of the ridge cap (constant along the length)
ROOF_RISE = 4.65  # rise of the ridge above the shoulder lines
T = 5.0           # wall thickness

SLOT_W = 12.0     # through slot in the front wall
SLOT_H = 2.5
SLOT_Z = 19.25    # slot centre height above the base

GROOVE_W = 12.0   # guide groove on the inside of the front wall,
GROOVE_D = 0.8    # from the open bottom edge up to the slot

# ---------------- derived ----------------
yf = -L / 2.0     # front face plane  (part runs along +Y, front at -Y)
yb = L / 2.0      # back face plane
EPS = 1e-6


def poly(pts):
    return cq.Wire.makePolygon([cq.Vector(*p) for p in pts], close=True)


def trapezoid(y, w, h):
    """Lower (tapering) part of the section at station y."""
    hs = h - ROOF_RISE  # shoulder height
    return poly([(-w / 2.0, y, 0.0), (w / 2.0, y, 0.0),
                 (ROOF_HALF, y, hs), (-ROOF_HALF, y, hs)])


def cap_triangle(y, h):
    """Ridge cap section at station y."""
    hs = h - ROOF_RISE
    return poly([(-ROOF_HALF, y, hs), (ROOF_HALF, y, hs), (0.0, y, h)])


# 1) tapered lower body: ruled loft between the front and back trapezoids
lower = cq.Solid.makeLoft([trapezoid(yf, W0, H0), trapezoid(yb, W1, H1)], ruled=True)

# 2) shell it inwards, leaving the bottom, the back end and the top strip open
#    (the top strip is closed again by the solid ridge cap)
open_faces = []
for f in lower.Faces():
    c = f.Center()
    n = f.normalAt(c)
    if abs(c.z) < EPS and n.z < -0.5:                 # bottom
        open_faces.append(f)
    elif abs(c.y - yb) < EPS and n.y > 0.5:           # back end
        open_faces.append(f)
    elif abs(c.x) < EPS and n.z > 0.5 and c.z > T:    # top strip (shoulder plane)
        open_faces.append(f)
walls = lower.shell(open_faces, -T)

# 3) solid ridge cap: constant triangular section swept straight along the
#    sloping ridge (its end faces stay vertical)
cap = cq.Solid.extrudeLinear(cq.Face.makeFromWires(cap_triangle(yf, H0)),
                             cq.Vector(0.0, L, H1 - H0))

body = cq.Workplane("XY").add(walls).union(cq.Workplane("XY").add(cap))

# 4) horizontal through slot in the front wall
slot = (cq.Workplane("XY")
        .box(SLOT_W, T + 2.0, SLOT_H)
        .translate((0.0, yf + T / 2.0, SLOT_Z)))
body = body.cut(slot)

# 5) shallow guide groove on the inner face of the front wall,
#    open at the bottom edge and running up into the slot
g_len = SLOT_Z + 1.0
groove = (cq.Workplane("XY")
          .box(GROOVE_W, GROOVE_D + 1.0, g_len)
          .translate((0.0, yf + T - GROOVE_D + (GROOVE_D + 1.0) / 2.0, g_len / 2.0 - 1.0)))
body = body.cut(groove)

result = body.solids()   # the single finished solid

VIEW = {"azimuth": 45, "elevation": 26}
